import math
import cadquery as cq

# Caster wheel: moulded tyre on a cast rim with a four-slot web, hub and
# flanged plain bushing.  Wheel axis = Y, symmetric about the XZ plane.

# ---------------- driving dimensions (mm) ----------------
TIRE_R_OUT = 98.6       # tread radius at the shoulders (before rounding)
TIRE_CROWN = 2.0        # extra radius at the tread centre
TIRE_R_IN = 82.0        # tyre seat radius = rim flange outer radius
TIRE_SIDE_TILT = 11.0   # mean lean of the side walls towards the tread (deg)
TIRE_SIDE_TILT0 = 4.0   # lean of the side walls where they leave the bead (deg)
TIRE_BEAD_R = 3.5       # concave blend of the tyre side into the rim flange
TIRE_SHOULDER_R = 6.0   # shoulder rounding

RIM_HW = 30.0           # half width of the rim flange faces
RIM_LIP_R = 72.4        # inner radius of the rim lip at the flange face
RIM_IN_R = 71.6         # inner radius of the rim just above the web blend
WEB_HW = 5.5            # half thickness of the web
RIM_WEB_R = 9.0         # large cast blend between rim and web

HUB_R = 40.0            # hub radius at the hub face
HUB_R_BACK = 41.8       # hub radius where it meets the web (cast draft)
HUB_HW = 32.6           # hub half length
HUB_WEB_R = 1.8         # blend between hub and web
HUB_EDGE_R = 0.8        # rounded outer edge of the hub faces

CB_R = 15.5             # counterbore in the hub faces
CB_D = 2.0
BUSH_FL_R = 14.2        # bushing collar radius
BUSH_FL_PROUD = 0.7     # collar proud of the hub face
BUSH_R = 12.6           # bushing body radius
BUSH_HW = 37.8          # bushing half length
BORE_R = 9.7            # bore radius
BUSH_CH = 0.4           # outer chamfer on the bushing ends
BORE_CH = 1.2           # lead-in chamfer of the bore

SLOT_RI = 46.4          # kidney slot inner radius
SLOT_RO = 67.2          # kidney slot outer radius
SLOT_HALF_ANG = 25.5    # angular half span of the slot centre line (deg)
SLOT_N = 4
SLOT_FILLET = 2.5       # small radius on the slot mouths


SEAM_ROT = 130.0        # park the revolve seams low at the back (cosmetic)


def revolve_y(wp):
    return wp.revolve(360, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 1, 0), SEAM_ROT)


def corner_arc(p_from, corner, p_to, rad):
    """Tangent arc replacing a sharp corner of a polyline.
    Returns (start, mid, end) of the arc."""
    ax, ay = p_from[0] - corner[0], p_from[1] - corner[1]
    bx, by = p_to[0] - corner[0], p_to[1] - corner[1]
    la, lb = math.hypot(ax, ay), math.hypot(bx, by)
    ax, ay, bx, by = ax / la, ay / la, bx / lb, by / lb
    cos_t = ax * bx + ay * by
    t = math.acos(max(-1.0, min(1.0, cos_t)))
    d = rad / math.tan(t / 2)
    s = (corner[0] + ax * d, corner[1] + ay * d)
    e = (corner[0] + bx * d, corner[1] + by * d)
    bis = (ax + bx, ay + by)
    lbis = math.hypot(*bis)
    h = rad / math.sin(t / 2)
    c = (corner[0] + bis[0] / lbis * h, corner[1] + bis[1] / lbis * h)
    m = (c[0] - bis[0] / lbis * rad, c[1] - bis[1] / lbis * rad)
    return s, m, e


def rounded_path(pts, radii):
    """pts: polyline corners; radii[i] = blend radius at pts[i] (0 = sharp).
    Returns list of segments: ('L', end) / ('A', mid, end), plus start point."""
    segs = []
    start = pts[0]
    for i in range(1, len(pts) - 1):
        r = radii[i]
        if r > 0:
            s, m, e = corner_arc(pts[i - 1], pts[i], pts[i + 1], r)
            segs.append(('L', s))
            segs.append(('A', m, e))
        else:
            segs.append(('L', pts[i]))
    segs.append(('L', pts[-1]))
    return start, segs


def mirrored_section(pts, radii):
    """Closed (r, y) section symmetric about y=0.  pts run from the axis side
    on +Y to the outer rim on +Y; the -Y half is the mirror image."""
    start, segs = rounded_path(pts, radii)
    wp = cq.Workplane("XY").moveTo(*start)
    for sg in segs:
        if sg[0] == 'L':
            wp = wp.lineTo(*sg[1])
        else:
            wp = wp.threePointArc(sg[1], sg[2])
    # walk back along the mirrored half
    nodes = [start] + [sg[-1] for sg in segs]
    mirrored = [(p[0], -p[1]) for p in nodes]
    wp = wp.lineTo(*mirrored[-1])
    for j in range(len(segs) - 1, -1, -1):
        sg = segs[j]
        target = mirrored[j]
        if sg[0] == 'L':
            wp = wp.lineTo(*target)
        else:
            wp = wp.threePointArc((sg[1][0], -sg[1][1]), target)
    return wp.close()


# ---------------- tyre ----------------
# section: crowned tread, rounded shoulders, gently convex side walls that
# lean in towards the shoulder, and a concave bead blend running into the rim
# flange corner.
b1 = math.radians(TIRE_SIDE_TILT0)                     # wall tilt at the bead
gam = math.radians(TIRE_SIDE_TILT)                     # mean (chord) tilt
bc = (TIRE_R_IN + TIRE_BEAD_R, RIM_HW)                 # bead blend centre
bp = (bc[0] - TIRE_BEAD_R * math.sin(b1),              # tangent point bead/wall
      bc[1] - TIRE_BEAD_R * math.cos(b1))
bm = (bc[0] - TIRE_BEAD_R * math.sin(math.pi / 4 + b1 / 2),
      bc[1] - TIRE_BEAD_R * math.cos(math.pi / 4 + b1 / 2))
shoulder_hw = bp[1] - (TIRE_R_OUT - bp[0]) * math.tan(gam)
sp = (TIRE_R_OUT, shoulder_hw)                          # raw shoulder corner
# convex side wall: a smooth curve leaving the bead blend tangentially with
# tilt TIRE_SIDE_TILT0 and reaching the shoulder corner with a steeper tilt so
# that its mean lean is TIRE_SIDE_TILT
b2 = 2 * gam - b1
crown_pt = (TIRE_R_OUT + TIRE_CROWN, 0.0)

tire_wp = (
    cq.Workplane("XY")
    .moveTo(TIRE_R_IN, -bc[1])
    .threePointArc((bm[0], -bm[1]), (bp[0], -bp[1]))
    .spline([(sp[0], -sp[1])], tangents=[(math.cos(b1), math.sin(b1)),
                                         (math.cos(b2), math.sin(b2))],
            includeCurrent=True)
    .threePointArc(crown_pt, sp)
    .spline([bp], tangents=[(-math.cos(b2), math.sin(b2)),
                            (-math.cos(b1), math.sin(b1))],
            includeCurrent=True)
    .threePointArc(bm, (TIRE_R_IN, bc[1]))
    .close()
)
tire_s = revolve_y(tire_wp).val()
shoulders = []
for e in tire_s.Edges():
    bb = e.BoundingBox()
    if abs(bb.xmax - TIRE_R_OUT) < 0.05 and abs(abs(bb.ymin) - shoulder_hw) < 0.05 \
            and abs(bb.ymax - bb.ymin) < 0.05:
        shoulders.append(e)
tire_s = tire_s.fillet(TIRE_SHOULDER_R, shoulders)
tire = cq.Workplane("XY").add(tire_s)

# ---------------- rim + web + hub (one casting) ----------------
rim_pts = [
    (CB_R, HUB_HW),
    (HUB_R, HUB_HW),            # rounded hub face edge
    (HUB_R_BACK, WEB_HW),       # hub / web blend
    (RIM_IN_R, WEB_HW),         # large rim / web blend
    (RIM_LIP_R, RIM_HW),        # sharp lip
    (TIRE_R_IN, RIM_HW),
]
rim_radii = [0, HUB_EDGE_R, HUB_WEB_R, RIM_WEB_R, 0, 0]
body_s = revolve_y(mirrored_section(rim_pts, rim_radii)).val()


# ---------------- kidney slots through the web ----------------
def arc_slot(ri, ro, half_ang_deg, length):
    a = math.radians(half_ang_deg)
    rm, w = (ri + ro) / 2, ro - ri
    # sketch on XZ plane: local x = global X, local y = global Z, normal = -Y
    po1 = (-ro * math.sin(a), ro * math.cos(a))
    po2 = (ro * math.sin(a), ro * math.cos(a))
    pi1 = (-ri * math.sin(a), ri * math.cos(a))
    pi2 = (ri * math.sin(a), ri * math.cos(a))
    c1 = (-rm * math.sin(a), rm * math.cos(a))
    c2 = (rm * math.sin(a), rm * math.cos(a))
    e2 = (c2[0] + (w / 2) * math.cos(a), c2[1] - (w / 2) * math.sin(a))
    e1 = (c1[0] - (w / 2) * math.cos(a), c1[1] - (w / 2) * math.sin(a))
    return (
        cq.Workplane("XZ", origin=(0, length / 2, 0))
        .moveTo(*po1)
        .threePointArc((0, ro), po2)
        .threePointArc(e2, pi2)
        .threePointArc((0, ri), pi1)
        .threePointArc(e1, po1)
        .close()
        .extrude(length)
    )


slots = None
for i in range(SLOT_N):
    s = arc_slot(SLOT_RI, SLOT_RO, SLOT_HALF_ANG, 2 * RIM_HW).rotate(
        (0, 0, 0), (0, 1, 0), i * 360.0 / SLOT_N)
    slots = s if slots is None else slots.union(s)

body_s = body_s.cut(slots.val())


def on_slot_outline(x, z, tol=1e-3):
    """True if (x, z) lies on the outline of one of the kidney slots."""
    a = math.radians(SLOT_HALF_ANG)
    rm, hw_ = (SLOT_RI + SLOT_RO) / 2, (SLOT_RO - SLOT_RI) / 2
    r = math.hypot(x, z)
    for i in range(SLOT_N):
        t = math.radians(i * 360.0 / SLOT_N)
        for sg in (1, -1):
            xl = x * math.cos(t) - sg * z * math.sin(t)
            zl = sg * x * math.sin(t) + z * math.cos(t)
            phi = math.atan2(xl, zl)
            if abs(phi) <= a + 1e-6 and (abs(r - SLOT_RI) < tol or abs(r - SLOT_RO) < tol):
                return True
            for sx in (-1, 1):
                cx, cz = sx * rm * math.sin(a), rm * math.cos(a)
                if abs(math.hypot(xl - cx, zl - cz) - hw_) < tol:
                    return True
    return False


# round the slot mouths on both sides of the web
if SLOT_FILLET > 0:
    slot_edges = []
    for e in body_s.Edges():
        p = e.positionAt(0.5)
        if abs(p.y) >= WEB_HW - 1e-4 and abs(p.y) < RIM_HW - 1e-3 \
                and on_slot_outline(p.x, p.z, 0.02):
            slot_edges.append(e)
    try:
        body_s = body_s.fillet(SLOT_FILLET, slot_edges)
    except Exception as ex:  # keep going with sharp slot edges
        print("slot fillet failed:", ex, len(slot_edges))
body = cq.Workplane("XY").add(body_s)

# ---------------- flanged bushing ----------------
bush_pts = [
    (BUSH_R - BUSH_CH, -BUSH_HW),
    (BUSH_R, -BUSH_HW + BUSH_CH),
    (BUSH_R, -HUB_HW - BUSH_FL_PROUD),
    (BUSH_FL_R, -HUB_HW - BUSH_FL_PROUD),
    (BUSH_FL_R, -HUB_HW + CB_D),
    (CB_R, -HUB_HW + CB_D),
    (CB_R, HUB_HW - CB_D),
    (BUSH_FL_R, HUB_HW - CB_D),
    (BUSH_FL_R, HUB_HW + BUSH_FL_PROUD),
    (BUSH_R, HUB_HW + BUSH_FL_PROUD),
    (BUSH_R, BUSH_HW - BUSH_CH),
    (BUSH_R - BUSH_CH, BUSH_HW),
    (BORE_R + BORE_CH, BUSH_HW),
    (BORE_R, BUSH_HW - BORE_CH),
    (BORE_R, -BUSH_HW + BORE_CH),
    (BORE_R + BORE_CH, -BUSH_HW),
]
bush = revolve_y(cq.Workplane("XY").polyline(bush_pts).close())

result = body.union(tire).union(bush)

VIEW = {"azimuth": 45, "elevation": 26}
